import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
# ring (hoop) lying in the XZ plane, centred on the origin
RING_RO = 59.4
RING_RI = 55.5
RING_W = 3.65          # thickness along Y

# U-bracket
L = 101.0              # overall length along X
HALF = L / 2.0
Z_TOP = 25.1
Y_FRONT = -14.8        # lip / rib front
Y_FACE = -12.25        # main front face
Y_BACK = -9.35         # back face of front wall
Z_WALL_BOT = -9.3      # bottom of the main wall (central opening)
LIP_Z0 = 21.9          # bottom of the top lip's front face
LIP_Z1 = 19.7          # end of the chamfer under the lip
RIB_Z = (3.2, 0.9, -2.35, -4.35)   # mid rib: chamfer start, front top, front bottom, chamfer end
LOW_CH = (-9.73, -12.0)            # chamfer onto the lower (knuckle) section

PLATE_T = 6.85         # end plate thickness (X)
PLATE_Y1 = 14.7        # back edge of end plates
PLATE_ZB = -4.7        # bottom of end plates
PLATE_HOLE_Y = 2.5
PLATE_HOLE_Z = 17.4
PLATE_HOLE_R = 3.6

# lower section / knuckles
LOW_Z = -15.4
LOW_YB = -9.35
CUT_HALF = 18.5        # half width of central opening
KN_Y = -8.55
KN_Z = -18.75
KN_R = 6.4
KN_HOLE_R = 3.65
KN_OUT_W = PLATE_T     # outer knuckles flush with the end plates
KN_IN_W = 4.8
FIN_TIP = (4.4, -15.0)  # rear tip of the knuckle gusset (Y, Z)
FIN_TOP = (1.6, -11.6)  # where the gusset upper edge ends
END_HOLE_Y = 2.5        # relief hole in the lower end region (along X)
END_HOLE_Z = -7.2
END_HOLE_R = 3.6

FRONT_HOLE_Z = 4.85
FRONT_HOLE_R = 2.9

# inner blocks
BLK_X0 = 16.25
BLK_X1 = 26.0
BLK_Y1 = 9.4
BLK_Z0 = -9.75
BLK_Z1 = 9.5
BLK_GUSSET = 4.5
BLK_HOLE_R = 2.2
BLK_SLOT_Z = -5.6
BLK_SLOT_H = 2.4
BLK_SLOT_D = 2.0
BLK_GROOVE_D = 1.2
BLK_HOLE_Z = 1.0

# pulley + roller on a Y axis through the origin
DISC_R = 14.6
DISC_Y0 = -3.9
DISC_Y1 = -1.6
HUB_R = 5.1           # boss on the pulley
HUB_Y0 = -6.1
STEM_R = 2.2          # axle stem into the wall
STEM_FLARE = 4.0
FLARE_LEN = 2.0
PLATE2_Y1 = -6.1      # stiffening plate between the inner blocks
PLATE2_Z1 = -3.5
ROLL_R = 5.8
ROLL_Y1 = 6.5
ROLL_Z = FRONT_HOLE_Z  # roller sits on the pin line of the front hole
DISC_RIM = 2.0        # width of the raised pulley rim
DISC_RECESS = 0.7
STRAP_Y0 = 1.85
STRAP_Y1 = 4.0
STRAP_HALF = 12.1
STRAP_ZB = -7.2
STRAP_ZT = 5.5
STRAP_T = 1.2
DISC_FILLET = 0.8


def yz_profile(pts, x0, length):
    """polygon given as (Y, Z) pairs, extruded along +X from x0"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close().extrude(length))


def x_cyl(y, z, r, x0, length, seam=(0, 0, 1)):
    """cylinder along +X starting at x0 (seam placed on a hidden side)"""
    pl = cq.Plane(origin=(x0, y, z), xDir=seam, normal=(1, 0, 0))
    return cq.Workplane(pl).circle(r).extrude(length)


def y_cyl(x, z, r, y0, length, seam=(-1, 0, 1)):
    """cylinder along +Y starting at y0 (seam placed on a hidden side)"""
    pl = cq.Plane(origin=(x, y0, z), xDir=seam, normal=(0, 1, 0))
    return cq.Workplane(pl).circle(r).extrude(length)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- ring ----------------
ring = (cq.Workplane("XZ", origin=(0, RING_W / 2.0, 0))
        .circle(RING_RO).circle(RING_RI).extrude(RING_W))

# ---------------- front wall ----------------
wall_pts = [
    (Y_FRONT, Z_TOP),
    (Y_FRONT, LIP_Z0),
    (Y_FACE, LIP_Z1),
    (Y_FACE, RIB_Z[0]),
    (Y_FRONT, RIB_Z[1]),
    (Y_FRONT, RIB_Z[2]),
    (Y_FACE, RIB_Z[3]),
    (Y_FACE, Z_WALL_BOT),
    (Y_BACK, Z_WALL_BOT),
    (Y_BACK, Z_TOP),
]
wall = yz_profile(wall_pts, -HALF, L)

# lower section (left and right of the central opening)
low_pts = [
    (Y_FACE, Z_WALL_BOT + 0.3),
    (Y_FACE, LOW_CH[0]),
    (Y_FRONT, LOW_CH[1]),
    (Y_FRONT, LOW_Z),
    (LOW_YB, LOW_Z),
    (LOW_YB, Z_WALL_BOT + 0.3),
]
low_len = HALF - CUT_HALF
lower = (yz_profile(low_pts, -HALF, low_len)
         .union(yz_profile(low_pts, CUT_HALF, low_len)))

# ---------------- end plates ----------------
plates = (box(-HALF, -HALF + PLATE_T, Y_BACK, PLATE_Y1, PLATE_ZB, Z_TOP)
          .union(box(HALF - PLATE_T, HALF, Y_BACK, PLATE_Y1, PLATE_ZB, Z_TOP)))

# ---------------- knuckles (lugs with a rear gusset) ----------------
# rear 45 deg edge tangent to the knuckle circle
_tx = KN_Y + KN_R * math.sqrt(0.5)
_tz = KN_Z - KN_R * math.sqrt(0.5)


def knuckle(x0, w, top_z, outer):
    pts = [(KN_Y, KN_Z), (KN_Y, LOW_Z + 0.5),
           (Y_BACK - 0.8, LOW_Z + 0.5), (Y_BACK - 0.8, top_z)]
    if outer:
        pts += [(END_HOLE_Y + 2.6, top_z)]
    else:
        pts += [(FIN_TOP[0] - 0.3, top_z)]
    pts += [FIN_TOP, FIN_TIP, (_tx, _tz)]
    lug = yz_profile(pts, x0, w).union(x_cyl(KN_Y, KN_Z, KN_R, x0, w))
    return lug


knuckles = (knuckle(-HALF, KN_OUT_W, PLATE_ZB + 0.01, True)
            .union(knuckle(HALF - KN_OUT_W, KN_OUT_W, PLATE_ZB + 0.01, True))
            .union(knuckle(-CUT_HALF - KN_IN_W, KN_IN_W, BLK_Z0 + 0.01, False))
            .union(knuckle(CUT_HALF, KN_IN_W, BLK_Z0 + 0.01, False)))

# ---------------- inner blocks ----------------
def block(sign):
    pts = [(BLK_X0, BLK_Y1), (BLK_X1, BLK_Y1),
           (BLK_X1, Y_BACK + BLK_GUSSET), (BLK_X1 + BLK_GUSSET, Y_BACK),
           (BLK_X0, Y_BACK)]
    pts = [(sign * x, y) for x, y in pts]
    if sign < 0:
        pts = pts[::-1]
    return (cq.Workplane("XY", origin=(0, 0, BLK_Z0))
            .polyline(pts).close().extrude(BLK_Z1 - BLK_Z0))


blocks = block(1).union(block(-1))

# ---------------- pulley / roller / strap ----------------
disc = y_cyl(0, 0, DISC_R, DISC_Y0, DISC_Y1 - DISC_Y0)
disc = disc.faces("|Y").edges().fillet(DISC_FILLET)
hub = y_cyl(0, 0, HUB_R, HUB_Y0, DISC_Y0 - HUB_Y0 + 0.02)
stem = y_cyl(0, 0, STEM_R, Y_BACK - 0.01, HUB_Y0 - Y_BACK + 0.05)
flare = cq.Solid.makeCone(STEM_FLARE, STEM_R, FLARE_LEN, cq.Vector(0, Y_BACK - 0.01, 0),
                          cq.Vector(0, 1, 0))
hub = hub.union(stem).union(cq.Workplane("XY").add(flare))
plate2 = box(-BLK_X0 - 0.01, BLK_X0 + 0.01, Y_BACK - 0.01, PLATE2_Y1,
             Z_WALL_BOT, PLATE2_Z1)
# shallow recess on the rear face of the pulley leaves a raised rim
recess = (cq.Workplane("XZ", origin=(0, DISC_Y1 + 0.01, 0))
          .circle(DISC_R - DISC_RIM).circle(HUB_R).extrude(DISC_RECESS + 0.01))
disc = disc.cut(recess)
roll = y_cyl(0, ROLL_Z, ROLL_R, DISC_Y1 - 0.5, ROLL_Y1 - DISC_Y1 + 0.5)
ball = cq.Workplane("XY").sphere(ROLL_R).translate((0, ROLL_Y1, ROLL_Z))
# U-strap (bail) around the roller, its arms resting on the pulley rim
strap = (box(-STRAP_HALF, STRAP_HALF, STRAP_Y0, STRAP_Y1,
             STRAP_ZB, STRAP_ZB + STRAP_T)
         .union(box(-STRAP_HALF, -STRAP_HALF + STRAP_T, DISC_Y1 - 0.2, STRAP_Y1,
                    STRAP_ZB, STRAP_ZT))
         .union(box(STRAP_HALF - STRAP_T, STRAP_HALF, DISC_Y1 - 0.2, STRAP_Y1,
                    STRAP_ZB, STRAP_ZT)))

body = (wall.union(lower).union(plates).union(knuckles).union(blocks)
        .union(disc).union(hub).union(roll).union(ball).union(strap)
        .union(plate2))

# ---------------- holes ----------------
body = body.cut(x_cyl(KN_Y, KN_Z, KN_HOLE_R, -HALF - 1, L + 2))
body = body.cut(x_cyl(PLATE_HOLE_Y, PLATE_HOLE_Z, PLATE_HOLE_R, -HALF - 1, L + 2))
# relief holes through the lower end regions
body = body.cut(x_cyl(END_HOLE_Y, END_HOLE_Z, END_HOLE_R, -HALF - 1, PLATE_T + 1))
body = body.cut(x_cyl(END_HOLE_Y, END_HOLE_Z, END_HOLE_R, HALF - PLATE_T, PLATE_T + 1))
# front hole along Y
body = body.cut(y_cyl(0, FRONT_HOLE_Z, FRONT_HOLE_R, Y_FRONT - 1, Y_BACK - Y_FRONT + 1.01))
# block cross holes along Y and the strap slot on their rear faces
for s in (-1, 1):
    xc = s * (BLK_X0 + BLK_X1) / 2.0
    body = body.cut(y_cyl(xc, BLK_HOLE_Z, BLK_HOLE_R, BLK_Y1 - 6.0, 6.5))
    xs_ = (s * (BLK_X0 - 0.1), s * (BLK_X1 - 2.0))
    body = body.cut(box(min(xs_), max(xs_),
                        BLK_Y1 - BLK_SLOT_D, BLK_Y1 + 0.1,
                        BLK_SLOT_Z - BLK_SLOT_H / 2, BLK_SLOT_Z + BLK_SLOT_H / 2))
    # the groove continues along the inner face of the block
    xg = (s * (BLK_X0 - 0.1), s * (BLK_X0 + BLK_GROOVE_D))
    body = body.cut(box(min(xg), max(xg), STRAP_Y0, BLK_Y1 + 0.1,
                        BLK_SLOT_Z - BLK_SLOT_H / 2, BLK_SLOT_Z + BLK_SLOT_H / 2))

result = body.union(ring)

VIEW = {"azimuth": 45, "elevation": 26}
